"""Hat-section tube bracket: a base plate with two mounting flanges and a
rectangular tunnel (tube) running front-to-back through the raised centre
section.  All top-side edges are blended except the front/back top edges of
the tower, which stay sharp."""
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
L = 80.0          # base length (X)
W = 40.0          # part depth (Y) - tunnel axis
TB = 7.5          # base plate thickness
H = 28.5          # overall height
TW = 40.0         # tower outer width (X)
HOLE_W = 29.0     # tunnel width (X)
HOLE_Z0 = 7.0     # tunnel floor height
HOLE_Z1 = 23.0    # tunnel ceiling height
R_TOP = 2.3       # convex fillet, tower top edges (along Y)
R_VERT = 2.2      # vertical tower corner edges (front/back)
R_ROOT = 3.0      # concave fillet, tower wall / flange (along Y)
R_FLANGE = 2.2    # flange top edges (ends and front/back)
D_HOLE = 9.0      # mounting hole diameter
HOLE_X = 30.0     # mounting hole offset from centre (X)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- hat profile in XZ, extruded along Y ----------------
pts = [
    (-L / 2, 0), (L / 2, 0), (L / 2, TB), (TW / 2, TB), (TW / 2, H),
    (-TW / 2, H), (-TW / 2, TB), (-L / 2, TB),
]
hat = (
    cq.Workplane("XZ")
    .polyline(pts).close()
    .extrude(W / 2, both=True)
)
solid = hat.val()

TOL = 1e-3


def near(a, b):
    return abs(a - b) < TOL


def radius_for(e):
    """Fillet radius for an edge of the sharp hat solid, or None to keep it sharp."""
    c = e.Center()
    bb = e.BoundingBox()
    dx, dy, dz = bb.xlen, bb.ylen, bb.zlen
    if dz > 1 and near(abs(c.x), TW / 2) and near(abs(c.y), W / 2):
        return R_VERT                      # vertical tower corners
    if dy > 1 and near(c.z, H) and near(abs(c.x), TW / 2):
        return R_TOP                       # tower top long edges
    if dy > 1 and near(c.z, TB) and near(abs(c.x), TW / 2):
        return R_ROOT                      # tower root (concave)
    if dy > 1 and near(c.z, TB) and near(abs(c.x), L / 2):
        return R_FLANGE                    # flange end top edges
    if dx > 1 and near(c.z, TB) and near(abs(c.y), W / 2):
        return R_FLANGE                    # flange front/back top edges
    return None


# all blends in one operation so that the tower's top front/back edges
# stay sharp (no tangent propagation around the top)
picked = [(radius_for(e), e) for e in solid.Edges()]
picked = [(r, e) for r, e in picked if r is not None]
mk = BRepFilletAPI_MakeFillet(solid.wrapped)
for r, e in picked:
    mk.Add(r, e.wrapped)
mk.Build()
if mk.IsDone():
    body = cq.Workplane("XY").newObject([cq.Shape.cast(mk.Shape())])
else:  # fallback: single radius through CadQuery
    body = hat.newObject([e for _, e in picked]).fillet(min(R_TOP, R_VERT, R_FLANGE))

# rectangular tunnel through along Y
tunnel = (
    cq.Workplane("XZ")
    .center(0, (HOLE_Z0 + HOLE_Z1) / 2)
    .rect(HOLE_W, HOLE_Z1 - HOLE_Z0)
    .extrude(W, both=True)
)
body = body.cut(tunnel)

# mounting holes through the flanges
holes = (
    cq.Workplane("XY")
    .pushPoints([(-HOLE_X, 0), (HOLE_X, 0)])
    .circle(D_HOLE / 2)
    .extrude(TB * 3)
    .translate((0, 0, -TB))
)
body = body.cut(holes)

result = body
